import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 64.4        # centre of side plates (+/-X)
PLATE_T = 3.8         # side plate thickness
PLATE_LEN = 140.0     # along Y
PLATE_H_END = 20.0    # height at the ends
PLATE_H_MID = 40.0    # height in the middle (right plate)
PLATE_H_MID_L = 38.0  # height in the middle (left plate)
PLATE_FLAT = 10.0     # half length of the arched middle part
ROD_R = 1.5           # threaded tie rods
NUT_R = 3.0
ROD_POS = [(5.0, 14.0), (-5.0, 14.0), (5.0, -14.0), (-5.0, -14.0), (64.5, -6.0), (-64.5, -6.0)]

DECK_X0, DECK_X1 = -56.5, -1.0
DECK_Y = 67.0
DECK_Z0, DECK_T = 0.0, 2.4

SERVO_X0, SERVO_X1 = -47.0, -9.0
SERVO_Y0, SERVO_Y1 = 8.5, 44.0
SERVO_W = 19.8
SHAFT_X = -18.6
EAR_L = 7.8
HORN_R_UP = 8.7       # horn disc on the upper servos
HORN_R_LOW = 7.0      # horn disc on the lower servos
ARCH_HW = 11.5        # half width of the bearing arches
ARCH_R = 11.0         # crown radius of the bearing arches
BOLT_DX = 8.7         # clamp bolts offset from the shaft
TUBE_H = 9.6          # bolt boss top above the shaft axis
ARCH_RI = 5.5         # inner radius of the bearing caps

FLOOR_X0, FLOOR_X1 = 0.0, 50.0
FLOOR_Y = 63.5
FLOOR_Z0, FLOOR_T = -11.9, 3.0

RS_X0, RS_X1 = 58.0, 95.0     # outboard servo body
RS_Y0, RS_Y1 = 8.0, 43.0
RS_Z0, RS_Z1 = -7.8, 11.6
RS_SHAFT_X = 86.0
RS_GUSSET_Y = (15.0, 32.0)

LINK_YS = [-59.0, -51.6, 55.4]
LINK_T = 3.4
LINK_PIN = (87.0, 2.0)

VIEW = {"azimuth": 45, "elevation": 26}


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0).translate(
        ((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2))


def cyl_x(x0, x1, y, z, r):
    return cq.Workplane("YZ").circle(r).extrude(x1 - x0).translate((x0, y, z))


def cyl_y(y0, y1, x, z, r):
    return cq.Workplane("XZ").circle(r).extrude(-(y1 - y0)).translate((x, y0, z))


def cyl_z(z0, z1, x, y, r):
    return cq.Workplane("XY").circle(r).extrude(z1 - z0).translate((x, y, z0))


def hex_x(x0, x1, y, z, r):
    return cq.Workplane("YZ").polygon(6, 2 * r).extrude(x1 - x0).translate((x0, y, z))


def bar_xz(p0, p1, w, y0, y1):
    """flat bar in the XZ plane from p0 to p1 (x, z), rounded ends, between y0 and y1."""
    dx, dz = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dz)
    ang = math.degrees(math.atan2(dz, dx))
    cx, cz = (p0[0] + p1[0]) / 2, (p0[1] + p1[1]) / 2
    return (cq.Workplane("XZ", origin=(0, y1, 0)).center(cx, cz)
            .slot2D(L + w, w, ang).extrude(y1 - y0))


def d_boss(ya, yb, xs, zc, r, x_back):
    """gear-train boss on the servo top: round around the shaft, straight towards x_back."""
    y0, y1 = min(ya, yb), max(ya, yb)
    c = cyl_y(y0, y1, xs, zc, r)
    b = box(min(xs, x_back), max(xs, x_back), y0, y1, zc - r, zc + r)
    return c.union(b)


def rounded_tab_y(x0, x1, y0, y1, z0, z1, top=True):
    """vertical tab in the XZ plane with a rounded end (top or bottom)."""
    w = x1 - x0
    r = w / 2
    if top:
        b = box(x0, x1, y0, y1, z0, z1 - r)
        c = cyl_y(y0, y1, (x0 + x1) / 2, z1 - r, r)
    else:
        b = box(x0, x1, y0, y1, z0 + r, z1)
        c = cyl_y(y0, y1, (x0 + x1) / 2, z0 + r, r)
    return b.union(c)


# ---------------- side plates ----------------
def plate_sketch(wp, h_mid):
    """elongated plate: straight tapers towards the ends, gentle arcs over the middle."""
    L = PLATE_LEN / 2
    he, hm, f = PLATE_H_END / 2, h_mid / 2, PLATE_FLAT
    sag = f * math.tan(math.atan((hm - he) / (L - f)) / 2)
    return (wp.moveTo(-L, -he).lineTo(-f, -hm + sag).threePointArc((0, -hm), (f, -hm + sag))
            .lineTo(L, -he).lineTo(L, he).lineTo(f, hm - sag).threePointArc((0, hm), (-f, hm - sag))
            .lineTo(-L, he).close())


def window_pts(sign):
    # tapered window, narrow at the outer end, wide towards the middle
    yo, yi = 46.0 * sign, 10.5 * sign
    return [(yo, -3.8), (yi, -8.0), (yi, 8.0), (yo, 3.8)]


def side_plate(x_c, h_mid, windows, servo_cut):
    wp = cq.Workplane("YZ", origin=(x_c - PLATE_T / 2, 0, 0))
    p = plate_sketch(wp, h_mid).extrude(PLATE_T)
    L = PLATE_LEN / 2
    p = p.edges("|X").edges(cq.selectors.BoxSelector((-100, -L - 1, -50), (100, -L + 1, 50))).fillet(3.0)
    p = p.edges("|X").edges(cq.selectors.BoxSelector((-100, L - 1, -50), (100, L + 1, 50))).fillet(3.0)
    for s in windows:
        w = (cq.Workplane("YZ", origin=(x_c - 5, 0, 0)).polyline(window_pts(s)).close()
             .extrude(10).edges("|X").fillet(3.0))
        p = p.cut(w)
    if servo_cut:
        p = p.cut(box(x_c - 5, x_c + 5, RS_Y0 - 0.5, RS_Y1 + 0.5, RS_Z0 - 0.5, RS_Z1 + 0.5))
    for (y, z) in ROD_POS:
        p = p.cut(cyl_x(x_c - 5, x_c + 5, y, z, ROD_R + 0.2))
    return p


left_plate = side_plate(-PLATE_X, PLATE_H_MID_L, [1, -1], False)
right_plate = side_plate(PLATE_X, PLATE_H_MID, [-1], True)

parts = [left_plate, right_plate]

# ---------------- rods: round heads on the left, nuts on the right ----------------
XO = PLATE_X + PLATE_T / 2
for (y, z) in ROD_POS:
    parts.append(cyl_x(-XO - 0.5, XO + 6.5, y, z, ROD_R))
    parts.append(cyl_x(-XO - 1.6, -XO, y, z, 2.7))          # button head
    if abs(y) > 30:
        parts.append(hex_x(XO, XO + 3.0, y, z, NUT_R))        # hex nut on the outer rods
    else:
        parts.append(cyl_x(XO, XO + 3.0, y, z, NUT_R))        # round nut
    parts.append(cyl_x(XO + 3.0, XO + 4.2, y, z, NUT_R - 0.8))
    parts.append(cyl_x(-XO + PLATE_T, SERVO_X0 - EAR_L, y, z, 2.2))   # spacer tube

# rod collars on the upper centre rods
for (x, y, z) in [(-51.0, 5.0, 14.0), (-51.0, -5.0, 14.0), (-5.0, 5.0, 14.0), (-5.0, -5.0, 14.0)]:
    parts.append(cyl_x(x - 2.0, x + 2.0, y, z, 2.6))
# clips joining the outer rods to the deck (above) and to the floor plate (below)
for sy in (-1, 1):
    for x in (-51.0, -5.0):
        c = cyl_x(x - 2.0, x + 2.0, sy * 64.5, -6.0, 2.6).union(
            box(x - 2.0, x + 2.0, sy * 64.5 - 2.0, sy * 64.5 + 2.0, -6.0, 0.5))
        parts.append(c)
    c = cyl_x(23.0, 27.0, sy * 64.5, -6.0, 2.6).union(
        box(23.0, 27.0, sy * 64.5 - 2.0, sy * 64.5 + 2.0, -12.6, -6.0)).union(
        box(23.0, 27.0, sy * 61.5, sy * 64.5, -12.6, -11.9) if sy > 0 else
        box(23.0, 27.0, sy * 64.5, sy * 61.5, -12.6, -11.9))
    parts.append(c)

# ---------------- servo deck ----------------
deck = (box(DECK_X0, DECK_X1, -DECK_Y, DECK_Y, DECK_Z0, DECK_Z0 + DECK_T)
        .edges("|Z").fillet(5.0).faces(">Z").edges().fillet(1.0))
# clearance slots for the output shafts between the bearing caps
for sy in (-1, 1):
    slot = (box(SHAFT_X - 13.2, SHAFT_X + 13.2, sy * 57.55 - 4.95, sy * 57.55 + 4.95, -5, 5)
            .edges("|Z").fillet(4.5))
    deck = deck.cut(slot)
parts.append(deck)


# ---------------- servos on the deck ----------------
def servo(ydir, upper):
    """servo lying on its side, length along X, width along Z, shaft along +/-Y."""
    if upper:
        z0, z1 = DECK_Z0 + DECK_T, DECK_Z0 + DECK_T + SERVO_W
    else:
        z0, z1 = DECK_Z0 - SERVO_W - 1.0, DECK_Z0
    zc = (z0 + z1) / 2
    y0, y1 = (SERVO_Y0, SERVO_Y1) if ydir > 0 else (-SERVO_Y1, -SERVO_Y0)
    body = box(SERVO_X0, SERVO_X1, y0, y1, z0, z1)
    # gear boss, output shaft and horn disc
    yt = y1 if ydir > 0 else y0
    boss = d_boss(yt, yt + 2.0 * ydir, SHAFT_X, zc, 7.0, SHAFT_X - 16.0)
    hr = HORN_R_UP if upper else HORN_R_LOW
    horn = cyl_y(min(yt + 2.0 * ydir, yt + 4.0 * ydir), max(yt + 2.0 * ydir, yt + 4.0 * ydir),
                 SHAFT_X, zc, hr)
    body = body.union(boss).union(horn)
    # mounting ears: tab with two holes + foot on the deck
    ey = (SERVO_Y1 - 7.0) if ydir > 0 else -(SERVO_Y1 - 7.0)
    for (ex0, ex1) in ((SERVO_X0 - EAR_L, SERVO_X0), (SERVO_X1, SERVO_X1 + EAR_L)):
        tab = rounded_tab_y(ex0, ex1, ey - 1.5, ey + 1.5, z0, z1, top=upper)
        ex = (ex0 + ex1) / 2
        for hz in (zc - 5.4, zc + 5.4):
            tab = tab.cut(cyl_y(ey - 3, ey + 3, ex, hz, 1.2))
        fy0, fy1 = (ey - 10.5, ey + 1.5) if ydir > 0 else (ey - 1.5, ey + 10.5)
        fz0, fz1 = (z0, z0 + 2.0) if upper else (z1 - 2.0, z1)
        foot = box(ex0, ex1, fy0, fy1, fz0, fz1)
        body = body.union(tab).union(foot)
    return body


for yd in (1, -1):
    for up in (True, False):
        parts.append(servo(yd, up))


# ---------------- shaft bearing blocks in front of the upper servos ----------------
def arch(y0, y1, zb, zc, solid):
    """bearing cap: half ring with hollow bolt bosses, on two posts (or on a solid pillow block)."""
    ring = cyl_y(y0, y1, SHAFT_X, zc, ARCH_R)
    ring = ring.intersect(box(SHAFT_X - ARCH_R - 1, SHAFT_X + ARCH_R + 1, y0, y1, zc, zc + ARCH_R + 1))
    if solid:
        ring = ring.union(box(SHAFT_X - ARCH_HW, SHAFT_X + ARCH_HW, y0, y1, zb, zc))
        ring = ring.union(box(SHAFT_X - ARCH_HW - 1.5, SHAFT_X + ARCH_HW + 1.5, y0, y1, zb, zc - 2.5))
    ring = ring.cut(cyl_y(y0 - 1, y1 + 1, SHAFT_X, zc, ARCH_RI))
    a = ring
    for bx in (SHAFT_X - BOLT_DX, SHAFT_X + BOLT_DX):
        a = a.union(box(bx - 2.6, bx + 2.6, y0, y1, zb, zc))                      # post
        t = cyl_z(zc - 3.0, zc + TUBE_H, bx, (y0 + y1) / 2, 2.1).faces(">Z").edges().fillet(0.9)
        t = t.cut(cyl_z(zc + TUBE_H - 2.0, zc + TUBE_H + 1, bx, (y0 + y1) / 2, 0.8))
        a = a.union(t)
    return a


def clamp(ydir):
    zb = DECK_Z0 + DECK_T
    zc = zb + SERVO_W / 2
    def yy(a, b):
        return (a, b) if ydir > 0 else (-b, -a)
    res = None
    for (a, b, solid) in ((49.0, 52.6, False), (62.5, 66.8, True)):
        y0, y1 = yy(a, b)
        p = arch(y0, y1, zb, zc, solid)
        res = p if res is None else res.union(p)
    return res


for yd in (1, -1):
    parts.append(clamp(yd))

# ---------------- floor plate ----------------
floor = (box(FLOOR_X0, FLOOR_X1, -FLOOR_Y, FLOOR_Y, FLOOR_Z0, FLOOR_Z0 + FLOOR_T)
         .edges("|Z").fillet(5.5).faces(">Z").edges().fillet(1.2))
parts.append(floor)

# ---------------- outboard servo on the right plate ----------------
rzc = (RS_Z0 + RS_Z1) / 2
rs = box(RS_X0, RS_X1, RS_Y0, RS_Y1, RS_Z0, RS_Z1)
rs = rs.union(d_boss(RS_Y0, RS_Y0 - 4.2, RS_SHAFT_X, rzc, 7.5, RS_X0 + 2.0))
rs = rs.union(cyl_y(RS_Y0 - 5.5, RS_Y0, RS_SHAFT_X, rzc, 4.2))
rs = rs.union(cyl_y(RS_Y0 - 7.5, RS_Y0, RS_SHAFT_X, rzc, 2.4))
for (ex0, ex1) in ((RS_X0 - 7.0, RS_X0), (RS_X1, RS_X1 + 6.0)):
    tab = box(ex0, ex1, RS_Y0 + 3.5, RS_Y0 + 12.0, RS_Z0, RS_Z1).edges("|Y").fillet(2.0)
    ex = (ex0 + ex1) / 2
    for hz in (rzc - 5.4, rzc + 5.4):
        tab = tab.cut(cyl_y(RS_Y0 + 2, RS_Y0 + 16, ex, hz, 1.3))
    rs = rs.union(tab)
# bent sheet bracket under the servo
rs = rs.union(box(XO, RS_X1 + 6.0, RS_Y0 - 2.0, RS_Y1 + 1.6, RS_Z0 - 1.8, RS_Z0))
rs = rs.union(box(XO, RS_X1 + 6.0, RS_Y1, RS_Y1 + 1.6, RS_Z0, RS_Z0 + 3.0))
# two diagonal gussets from the plate bottom to the bracket end
for gy in RS_GUSSET_Y:
    g = (cq.Workplane("XZ", origin=(0, gy + 1.1, 0))
         .polyline([(XO, -19.3), (XO, RS_Z0 - 1.8), (RS_X1 + 6.0, RS_Z0 - 1.8), (RS_X1 + 6.0, RS_Z0 - 4.2)])
         .close().extrude(2.2))
    rs = rs.union(g)
parts.append(rs)


# ---------------- A-frame links on the outer face of the right plate ----------------
def link(y_c):
    y0, y1 = y_c - LINK_T / 2, y_c + LINK_T / 2
    top_z = 12.5 - (abs(y_c) - 50.0) * 0.17
    a = bar_xz((XO + 1.0, top_z - 3.0), LINK_PIN, 6.0, y0, y1)
    b = bar_xz((XO + 1.0, -6.0), LINK_PIN, 4.5, y0, y1)
    return a.union(b)


for yc in LINK_YS:
    parts.append(link(yc))
# pins through the link eyes, with small heads
for (pa, pb) in ((-61.7, -48.9), (52.7, 58.1)):
    parts.append(cyl_y(pa, pb, LINK_PIN[0], LINK_PIN[1], 1.3))
    parts.append(cyl_y(pa - 0.6, pa, LINK_PIN[0], LINK_PIN[1], 1.9))
    parts.append(cyl_y(pb, pb + 0.6, LINK_PIN[0], LINK_PIN[1], 1.9))

result = parts[0]
for p in parts[1:]:
    result = result.union(p)
